import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Split-keyboard key-plate frame (Dactyl style): flat perimeter rim in the XZ
# plane (front face at Y=0), six curved, tented key columns standing off in +Y,
# and a raised, tilted three-key thumb cluster with a hood at the upper left.
# X: left -> right, Z: bottom -> top, Y: depth (keycap side is +Y).
# ---------------------------------------------------------------------------

RIM_W = 5.5          # rim band width
RIM_T = 6.0          # rim depth (Y)
RIM_FILLET = 1.5     # round on the rim's front edges
LEFT_RIM_X = 22.5    # inner edge of the (wider) left rim
PLATE_T = 5.0        # column key plate thickness
THUMB_T = 5.0        # thumb key plate thickness
HOLE = 14.0          # switch hole
ROW_PITCH = 25.5     # row pitch (along the column arc)
COL_R = 160.0        # column curvature radius
WALL_T = 3.0         # wall thickness
SCREW_D = 3.2
BOSS_D = 9.0
PORT_D = 19.0        # round port in the left hood wall
PORT_C = (22.5, 23.0, 87.0)  # port centre (X, Y, Z)
LW_Z0 = 60.0         # lower edge of the hood side wall

# frame outline seen from the front: sharp corner points (X, Z) and the
# fillet radius rounding each corner
OUTLINE_R = [
    (-1.4, 119.5, 7.0), (14.9, 143.3, 9.0), (45.9, 119.9, 10.0), (74.0, 113.8, 5.0),
    (83.9, 98.1, 6.0), (111.4, 97.5, 4.0), (117.0, 108.4, 4.0), (170.7, 108.4, 7.0),
    (170.7, 18.4, 7.0), (133.2, 17.6, 5.0), (118.8, 4.6, 6.0), (71.0, -0.25, 10.0),
    (61.5, 3.5, 6.0), (15.0, 3.5, 9.0), (15.5, 91.0, 8.0),
]


def rounded_path(wp, pts):
    """closed path through sharp corners (x, y, r) with each corner rounded
    by a tangent arc of radius r"""
    n = len(pts)
    segs = []
    for i in range(n):
        x0, y0, _ = pts[i - 1]
        x1, y1, r = pts[i]
        x2, y2, _ = pts[(i + 1) % n]
        d1 = (x1 - x0, y1 - y0)
        d2 = (x2 - x1, y2 - y1)
        l1, l2 = math.hypot(*d1), math.hypot(*d2)
        u1 = (d1[0] / l1, d1[1] / l1)
        u2 = (d2[0] / l2, d2[1] / l2)
        cosang = -(u1[0] * u2[0] + u1[1] * u2[1])
        half = math.acos(max(-1.0, min(1.0, cosang))) / 2
        d = min(r / math.tan(half), 0.45 * l1, 0.45 * l2)
        rr = d * math.tan(half)
        t1 = (x1 - u1[0] * d, y1 - u1[1] * d)
        t2 = (x1 + u2[0] * d, y1 + u2[1] * d)
        bx, by = u2[0] - u1[0], u2[1] - u1[1]
        bl = math.hypot(bx, by)
        k = rr / math.sin(half) - rr
        m = (x1 + bx / bl * k, y1 + by / bl * k)
        segs.append((t1, m, t2))
    wp = wp.moveTo(*segs[0][2])
    for i in range(1, n + 1):
        t1, m, t2 = segs[i % n]
        wp = wp.lineTo(*t1).threePointArc(m, t2)
    return wp.close()


def outline_prism(y_back, depth, inset=0.0):
    """prism of the (optionally inset) outline from Y=y_back towards -Y"""
    wp = rounded_path(cq.Workplane("XZ", origin=(0, y_back, 0)), OUTLINE_R)
    if inset:
        wp = wp.offset2D(-inset)
    return wp.extrude(depth)


# region (X, Z) where the rim is reduced to a thin lip under the hood
HOOD_RIM_CUT = [(-5.0, 112.0), (0.8, 113.0), (7.0, 127.0), (16.0, 133.0), (45.0, 116.0),
                (74.0, 108.5), (80.0, 108.5), (80.0, 150.0), (-5.0, 150.0)]
HOOD_LIP = 1.5

# screw bosses (X, Z) on the inner edge of the rim
SCREWS = [(24.4, 72.3), (24.3, 46.3), (64.2, 13.0), (72.7, 97.4),
          (161.1, 100.3), (122.5, 19.8)]

# columns: (x centre, z centre, y of key face at centre, tent deg, width)
COLUMNS = [
    (35.6, 49.5, 31.5, 20.0, 22.0),
    (57.9, 49.5, 22.5, 20.0, 22.0),
    (79.7, 46.8, 12.0, 10.0, 23.0),
    (105.4, 50.4, 12.0, 5.0, 24.0),
    (130.8, 63.0, 15.0, 0.0, 23.0),
    (154.7, 63.0, 15.0, 0.0, 23.0),
]
COL_HALF_LEN = 40.5
WEBS = [1, 2, 3]     # column pairs (i, i+1) joined by a stepped web
# rim heights each column's rounded top / bottom lip rolls onto (None = the
# plate just stops: under the thumb cluster)
COL_RIMS = [(None, 3.5), (None, 3.5), (97.5, 0.8), (97.5, 3.0), (108.4, 17.6), (108.4, 18.4)]
LIP_R = 11.0


# thumb cluster: three keys on an arc. Key-face centres, in-plane rotation
# (deg, seen from the front), and each key plate's extent along its own long
# axis (the plate carries on past the outer keys)
TH_KEYS = [((19.0, 20.8, 119.9), 37.0, (-10.4, 12.9)),
           ((37.3, 31.3, 109.3), 22.0, (-12.9, 12.9)),
           ((60.4, 41.8, 103.1), 13.0, (-12.9, 8.6))]
TH_RISE = 0.47                 # dY per unit of in-plane run along the arc
TH_S = (-0.469, 0.239, -0.850) # approximate "down the plate" direction
TH_WT, TH_WB = 12.0, 11.0      # plate extent along -S (upper) and +S (lower)
# rim points (X, Z) the hood rises from: left end, top corner, over the keys
HOOD_EDGE = [(0.6, 119.4), (15.8, 138.6), (34.0, 128.4), (53.5, 117.6), (73.5, 113.0)]
HOOD_CROWN = 2.5               # outward bulge of the hood half way back


def V(*a):
    return cq.Vector(*a)


def tup(v):
    return (v.x, v.y, v.z)


def vol(w):
    return sum(abs(v.Volume()) for v in w.solids().vals())


def safe_union(a, b):
    """boolean union that falls back to 'a' if the kernel returns a broken result"""
    try:
        r = a.union(b)
        va, vb, vr = vol(a), vol(b), vol(r)
        if 0.98 * va <= vr <= 1.02 * (va + vb) and all(v.isValid() for v in r.solids().vals()):
            return r
    except Exception:
        pass
    return a


# everything stays behind the front face and inside the rim outline
CLIP = outline_prism(100.0, 100.0)


def clipped(w):
    return w.intersect(CLIP)


# ----------------------------------------------------------------- frame rim
def frame():
    outer = outline_prism(RIM_T, RIM_T)
    inner = outline_prism(RIM_T + 1, RIM_T + 2, RIM_W)
    f = outer.cut(inner)
    try:
        f = f.faces("<Y").edges().fillet(RIM_FILLET)
    except Exception:
        pass
    # the left rim is wider
    f = f.union(cq.Workplane("XY").box(LEFT_RIM_X - 16.0, RIM_T, 80.0)
                .translate(((LEFT_RIM_X + 16.0) / 2, RIM_T / 2, 50.0)))
    for (x, z) in SCREWS:
        boss = cq.Workplane("XZ", origin=(x, RIM_T, z)).circle(BOSS_D / 2).extrude(RIM_T)
        f = f.union(boss)
    # web tying the upper-middle screw boss to the rim
    f = f.union(cq.Workplane("XY").box(16, RIM_T, 7).translate((79.0, RIM_T / 2, 97.5)))
    for (x, z) in SCREWS:
        hole = cq.Workplane("XZ", origin=(x, RIM_T + 1, z)).circle(SCREW_D / 2).extrude(RIM_T + 2)
        f = f.cut(hole)
    # under the thumb hood the rim is only a thin front lip; the hood shell
    # carries on from it
    cut = (cq.Workplane("XZ", origin=(0, RIM_T + 1, 0))
           .polyline(HOOD_RIM_CUT).close().extrude(RIM_T + 1 - HOOD_LIP))
    return f.cut(cut)


# ------------------------------------------------------------- key columns
def col_ends(i):
    """absolute heights of the bottom and top ends of column i's plate"""
    zc = COLUMNS[i][1]
    rt, rb = COL_RIMS[i]
    ht = COL_HALF_LEN if rt is None else rt - LIP_R - zc
    hb = COL_HALF_LEN if rb is None else zc - rb - LIP_R
    return zc - hb, zc + ht


def col_edge(i, side, z):
    """key-face edge point of column i at absolute height z; side -1 left, +1 right"""
    xc, zc, yk, tent, w = COLUMNS[i]
    t = math.radians(tent)
    dz = z - zc
    s = COL_R - math.sqrt(COL_R ** 2 - dz ** 2)
    x = side * w / 2
    return (xc + x * math.cos(t) + s * math.sin(t), yk - x * math.sin(t) + s * math.cos(t), z)


def column(xc, zc, yk, tent, w, rim_top=None, rim_bot=None):
    """curved key column with three switch holes. At an end given a rim
    height the plate rolls forward over a rounded lip (radius LIP_R) and runs
    flat onto the rim; otherwise it stops at COL_HALF_LEN."""
    R = COL_R
    ht = COL_HALF_LEN if rim_top is None else rim_top - LIP_R - zc
    hb = COL_HALF_LEN if rim_bot is None else zc - rim_bot - LIP_R
    a_t, a_b = math.asin(ht / R), -math.asin(hb / R)
    yc = yk + R  # curvature centre (Y)

    def p(r, a):
        return (yc - r * math.cos(a), r * math.sin(a))

    ro = R + PLATE_T
    am_ = (a_t + a_b) / 2
    prof = (cq.Workplane("YZ", origin=(-w / 2, 0, 0))
            .moveTo(*p(R, a_b)).threePointArc(p(R, am_), p(R, a_t))
            .lineTo(*p(ro, a_t)).threePointArc(p(ro, am_), p(ro, a_b)).close()
            .extrude(w))
    for k in (-1, 0, 1):
        a = k * ROW_PITCH / R
        hbx = cq.Workplane("XY").box(HOLE, 20.0, HOLE).translate((0, yk - PLATE_T / 2, 0))
        hbx = hbx.rotate((0, yc, 0), (1, yc, 0), -math.degrees(a))
        prof = prof.cut(hbx)
    c = prof
    t = PLATE_T
    r = LIP_R
    for end, sgn in ((rim_top, 1.0), (rim_bot, -1.0)):
        if end is None:
            continue
        ye, ze = p(R, a_t if sgn > 0 else a_b)
        # quarter ring from the plate end round to the horizontal, then flat
        # forward onto the rim
        oy, oz = ye - r, ze
        ri = r - t
        q = math.sqrt(0.5)
        pts_o = [(ye, ze), (oy + r * q, oz + sgn * r * q), (oy, oz + sgn * r)]
        pts_i = [(oy, oz + sgn * ri), (oy + ri * q, oz + sgn * ri * q), (ye - t, ze)]
        lip = (cq.Workplane("YZ", origin=(-w / 2, 0, 0))
               .moveTo(*pts_o[0]).threePointArc(pts_o[1], pts_o[2])
               .lineTo(-6.0, oz + sgn * r).lineTo(-6.0, oz + sgn * ri)
               .lineTo(*pts_i[0]).threePointArc(pts_i[1], pts_i[2]).close()
               .extrude(w))
        c = c.union(lip)
    c = c.rotate((0, yk, 0), (0, yk, 1), -tent)
    return c.translate((xc, 0, zc))


def quad_loft(pairs, t, down=True, smooth=True):
    """wall lofted through thin planar quads; each quad spans a->b and is
    thickened by t horizontally, perpendicular to a->b (towards -Y if
    'down', else towards +X)"""
    def build(rev):
        ws = []
        for a, b in pairs:
            a, b = V(*a), V(*b)
            n = (b - a).cross(V(0, 0, 1))
            n = V(n.x, n.y, 0).normalized()
            if (down and n.y > 0) or (not down and n.x < 0):
                n = -n
            n = n * t
            pts = [a, b, b + n, a + n]
            if rev:
                pts.reverse()
            ws.append(cq.Wire.makePolygon(pts, close=True))
        return cq.Solid.makeLoft(ws, not smooth)
    sol = build(False)
    if sol.Volume() < 0:
        sol = build(True)
    return cq.Workplane("XY").add(sol)


def web(i):
    """web joining the right edge of column i to the left edge of column i+1"""
    za = max(col_ends(i)[0], col_ends(i + 1)[0]) + 2
    zb = min(col_ends(i)[1], col_ends(i + 1)[1]) - 2
    pairs = []
    for k in range(5):
        z = za + (zb - za) * k / 4
        a = col_edge(i, 1, z)
        b = col_edge(i + 1, -1, z)
        pairs.append((a, b))
    return quad_loft(pairs, PLATE_T, down=True)


# -------------------------------------------------------------- thumb cluster
def key_axes(k):
    """long axis L, down-the-plate axis S and key-face normal N of thumb key k"""
    a = math.radians(TH_KEYS[k][1])
    L = V(math.cos(a), TH_RISE, -math.sin(a)).normalized()
    S = V(*TH_S)
    S = (S - L * S.dot(L)).normalized()
    N = L.cross(S).normalized()
    if N.y < 0:
        N = -N
    return L, S, N


def key_pt(k, a, b):
    L, S, N = key_axes(k)
    return V(*TH_KEYS[k][0]) + L * a + S * b


def th_pt(a, b):
    """point on the thumb plate; a < 0 refers to the left key, else the right"""
    k = 0 if a < 0 else 2
    return tup(key_pt(k, a, b))


def slab(p1, p2, q1, q2, t, inside):
    """thin ruled wall from base edge p1-p2 to top edge q1-q2, thickness t,
    thickened towards the point 'inside'"""
    p1, p2, q1, q2 = V(*p1), V(*p2), V(*q1), V(*q2)
    n = (p2 - p1).cross(q1 - p1).normalized()
    if n.dot(V(*inside) - p1) < 0:
        n = -n
    n = n * t
    w1 = cq.Wire.makePolygon([p1, p2, p2 + n, p1 + n], close=True)
    w2 = cq.Wire.makePolygon([q1, q2, q2 + n, q1 + n], close=True)
    return cq.Workplane("XY").add(cq.Solid.makeLoft([w1, w2], True))


def thumb():
    plate = None
    for k, (c, ang, (l0, l1)) in enumerate(TH_KEYS):
        L, S, N = key_axes(k)
        C = V(*c)
        pl = cq.Plane(origin=tup(C - N * THUMB_T), xDir=tup(L), normal=tup(N))
        p = (cq.Workplane(pl).center((l0 + l1) / 2, (TH_WB - TH_WT) / 2)
             .rect(l1 - l0, TH_WT + TH_WB).extrude(THUMB_T))
        pl2 = cq.Plane(origin=tup(C - N * (THUMB_T + 5)), xDir=tup(L), normal=tup(N))
        p = p.cut(cq.Workplane(pl2).rect(HOLE, HOLE).extrude(THUMB_T + 10))
        plate = p if plate is None else plate.union(p)

    # hood: shell from the rim's upper-left edge back to the plate's left end
    # and upper edge, built as one crowned slab per edge segment
    t = WALL_T
    y0 = 0.5
    f = HOOD_EDGE
    L0, S0, _ = key_axes(0)
    L1, S1, _ = key_axes(1)
    L2, S2, _ = key_axes(2)
    l00 = TH_KEYS[0][2][0]
    l21 = TH_KEYS[2][2][1]
    q = [key_pt(0, l00, TH_WB),
         key_pt(0, l00, -TH_WT),
         (key_pt(0, TH_KEYS[0][2][1], -TH_WT) + key_pt(1, TH_KEYS[1][2][0], -TH_WT)) * 0.5,
         (key_pt(1, TH_KEYS[1][2][1], -TH_WT) + key_pt(2, TH_KEYS[2][2][0], -TH_WT)) * 0.5,
         key_pt(2, l21, -TH_WT)]
    # inward directions along the plate for each hood segment
    q_in = [L0, S0, (S0 + S1).normalized(), (S1 + S2).normalized()]
    p = [V(x, y0, z) for x, z in f]
    up = [V(-0.75, 0.25, 0.6)] + [V(0.0, 0.45, 0.9)] * (len(f) - 1)
    up = [u.normalized() for u in up]
    c = [p[i] * 0.65 + q[i] * 0.35 + up[i] * HOOD_CROWN for i in range(len(f))]
    hood = None
    for i in range(len(f) - 1):
        # base offset: in the XZ plane, perpendicular to the rim segment, inwards
        d = p[i + 1] - p[i]
        nb = V(-d.z, 0, d.x).normalized()
        if nb.dot(V(40.0, y0, 100.0) - p[i]) < 0:
            nb = -nb
        nt = q_in[i] * t
        nb = nb * t
        nm = (nb + nt) * 0.5
        ws = [cq.Wire.makePolygon([a, b, b + o, a + o], close=True)
              for a, b, o in ((p[i], p[i + 1], nb), (c[i], c[i + 1], nm), (q[i], q[i + 1], nt))]
        seg = cq.Solid.makeLoft(ws, False)
        if not seg.isValid() or seg.Volume() <= 0:
            seg = cq.Solid.makeLoft([ws[0], ws[2]], True)
        seg = cq.Workplane("XY").add(seg)
        hood = seg if hood is None else safe_union(hood, seg)
    return safe_union(plate, hood)


def offset_polyline(pts, t, inside):
    """offset an open 2D polyline by t towards the side of point 'inside'
    (mitred joints)"""
    def nrm(a, b):
        dx, dz = b[0] - a[0], b[1] - a[1]
        l = math.hypot(dx, dz)
        return (-dz / l, dx / l)
    ns = [nrm(pts[i], pts[i + 1]) for i in range(len(pts) - 1)]
    mx = sum(p[0] for p in pts) / len(pts)
    mz = sum(p[1] for p in pts) / len(pts)
    sgn = 1.0 if (ns[0][0] * (inside[0] - pts[0][0]) + ns[0][1] * (inside[1] - pts[0][1])) > 0 else -1.0
    ns = [(sgn * a, sgn * b) for a, b in ns]
    out = []
    for i, p in enumerate(pts):
        if i == 0:
            n = ns[0]
            out.append((p[0] + n[0] * t, p[1] + n[1] * t))
        elif i == len(pts) - 1:
            n = ns[-1]
            out.append((p[0] + n[0] * t, p[1] + n[1] * t))
        else:
            a, b = ns[i - 1], ns[i]
            m = (a[0] + b[0], a[1] + b[1])
            ml = math.hypot(*m)
            m = (m[0] / ml, m[1] / ml)
            k = t / (m[0] * a[0] + m[1] * a[1])
            out.append((p[0] + m[0] * k, p[1] + m[1] * k))
    return out


def left_wall():
    """slanted outer side wall of the hood: from the rim's outer left edge back
    to column 1's outer edge, rising into the lower-left corner of the thumb
    plate; carries a round port"""
    y0 = 0.3
    pairs = []
    for z in (LW_Z0, 75.0, 89.0):
        e = col_edge(0, -1, z)
        pairs.append(((15.3, y0, z), (e[0] + 0.5, e[1], z)))
    c1 = V(*col_edge(0, -1, 89.0))
    bl = key_pt(0, TH_KEYS[0][2][0] + 1.0, TH_WB - 1.0)
    m = c1 + (bl - c1) * 0.47
    pairs.append(((11.6, y0, m.z), (m.x, m.y, m.z)))
    pairs.append(((1.2, y0, 115.5), (bl.x, bl.y, bl.z)))
    w = quad_loft(pairs, WALL_T, down=False)
    nrm = V(0.96, -0.28, 0)
    c = V(PORT_C[0], PORT_C[1], PORT_C[2]) - nrm * 10
    port = (cq.Workplane(cq.Plane(origin=tup(c), xDir=(0, 0, 1), normal=tup(nrm)))
            .circle(PORT_D / 2).extrude(20))
    return w.cut(port)


# ------------------------------------------------------------------ assembly
parts = frame()
for col, (rt, rb) in zip(COLUMNS, COL_RIMS):
    parts = safe_union(parts, clipped(column(*col, rim_top=rt, rim_bot=rb)))
for i in WEBS:
    parts = safe_union(parts, clipped(web(i)))
parts = safe_union(parts, clipped(left_wall()))
parts = safe_union(parts, clipped(thumb()))
result = parts
